import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
CUBE = 25.0            # cube edge length
PITCH = 75.0           # centre-to-centre distance hub cube -> arm cubes
BAR = 9.8              # side of the square bar (set on edge -> diamond section)
TIP = 6.9              # height of the pyramid point at each bar end
BAR_START = 13.2       # prism starts this far from the hub centre (0.7 mm clear of hub face)
BAR_LEN = 49.9         # prism length (runs 0.6 mm into the arm cube)
INSET = 0.5            # bar axis sits this far inside the cube edge
FILLET = 0.6           # cube edge round

h = CUBE / 2.0
e = h - INSET          # bar axis offset from the cube centre lines
r2 = 1.0 / math.sqrt(2.0)


def cube_at(x, y, z):
    """Cube with all edges rounded, centred at (x, y, z)."""
    return (cq.Workplane("XY").box(CUBE, CUBE, CUBE)
            .edges().fillet(FILLET)
            .translate((x, y, z)))


def pointed_bar():
    """Square bar standing on edge (diamond section, faces at 45 deg to X/Y),
    running along +Z from z=0 to z=BAR_LEN, with a four-sided pyramid point
    of height TIP at each end.  Built as the intersection of two pointed
    side-profiles extruded at right angles to each other."""
    a = BAR / 2.0
    prof = [(0.0, -TIP), (a, 0.0), (a, BAR_LEN), (0.0, BAR_LEN + TIP),
            (-a, BAR_LEN), (-a, 0.0)]
    p = cq.Vector(r2, r2, 0)      # across one pair of faces
    q = cq.Vector(r2, -r2, 0)     # across the other pair
    wp1 = cq.Workplane(cq.Plane(origin=(0, 0, 0), xDir=p, normal=q))
    wp2 = cq.Workplane(cq.Plane(origin=(0, 0, 0), xDir=q, normal=-p))
    s1 = wp1.polyline(prof).close().extrude(a, both=True)
    s2 = wp2.polyline(prof).close().extrude(a, both=True)
    return s1.intersect(s2)


O = (0, 0, 0)

# hub cube at the origin, arm cubes along +X, +Y, +Z
body = (cube_at(0, 0, 0)
        .union(cube_at(PITCH, 0, 0))
        .union(cube_at(0, PITCH, 0))
        .union(cube_at(0, 0, PITCH)))

# vertical bar on the hub's (-X,-Y) edge: hub -> top cube
bar_z = pointed_bar().translate((-e, -e, BAR_START))
# bar along X on the (-Y,-Z) edge: hub -> +X cube
bar_x = (pointed_bar().rotate(O, (0, 1, 0), 90)
         .translate((BAR_START, -e, -e)))
# bar along Y on the (-X,-Z) edge: hub -> +Y cube
bar_y = (pointed_bar().rotate(O, (1, 0, 0), -90)
         .translate((-e, BAR_START, -e)))

result = body.union(bar_z).union(bar_x).union(bar_y)

VIEW = {"azimuth": 45, "elevation": 26}
